import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Vertical belt-driven linear axis with gear motor, tensioner block and
# side mounting plates.  Z is the axis direction, units: mm.
# ---------------------------------------------------------------------------

H_TOTAL = 1433.0          # overall height (bottom dome to top dome)

# end caps (drive head on top, idler head at bottom)
CAP_X = 87.0              # width in X
CAP_Y = 101.0             # depth in Y
BOT_BODY_H, BOT_DOME_H = 99.0, 17.0    # idler head (bottom)
TOP_BODY_H, TOP_DOME_H = 106.0, 22.0   # drive head (top)
BOT_SHAFT_U = 44.0        # shaft axis distance from the outer end of the block
TOP_SHAFT_U = 48.0
RECESS_U0, RECESS_U1 = 5.0, 80.0     # recess on -Y face, from block outer end
RECESS_X0, RECESS_X1 = -27.0, 25.0
RECESS_D = 5.0
FL_R = 27.0               # bearing flange disc radius
FL_LUG_R = 0.0            # screw lug radius (0: plain disc)
SHAFT_Y = 3.0             # pulley shaft offset in Y
FL_BOLT_R = 33.0          # flange screw circle radius
CAP_TOP_CHAMFER = 2.5     # bevel around the outer end of the head blocks
CAP_SCREW_X, CAP_SCREW_Y = 34.0, 40.0   # corner screws on the outer face
DOME_Y0, DOME_Y1 = -50.5, 42.0          # pulley cover extent in Y
DOME_BAND_X = 18.8                      # half width of the central band
DOME_WIDE_Y = (-26.0, 26.7)             # full-width part of the cover
FL_BOSS_R = 12.0          # bearing boss radius

# aluminium profile
PROF_X0, PROF_X1 = -44.0, 40.0
PROF_Y0, PROF_Y1 = -49.0, 38.0
PROF_CHAMFER = 9.0                   # bevels on the rear corners
PROF_FRONT_CHX, PROF_FRONT_CHY = 2.0, 2.0
GROOVE_W = 6.0
GROOVE_D = 4.0
FRONT_GROOVE_X = 30.0
PX_GROOVES = ((0.5, 4.0), (13.5, 6.0))    # +X face grooves (y centre, width)
MX_GROOVES = ((-1.0, 4.0),)                # -X face grooves
REAR_SLOTS = ((9.0, 27.0, 8.0), (-33.0, -25.0, 5.0))  # +Y face (x0, x1, depth)

Z_PROF0 = BOT_BODY_H + BOT_DOME_H
Z_PROF1 = H_TOTAL - (TOP_BODY_H + TOP_DOME_H)

# mounting plate (front, -Y side)
PLATE_T = 8.5
PLATE_X0, PLATE_X1 = -188.0, -16.0
PLATE_Z0, PLATE_Z1 = 1103.0, 1251.0
BRK_X0, BRK_X1 = -118.0, -19.0
BRK_Z0, BRK_Z1 = 1022.0, 1084.0

# tensioner block on +Y side of the drive head
TB_X = 94.0
TB_Y0, TB_Y1 = 50.5, 100.0
TB_Z0 = 1334.0
TP_Z1 = 1418.0            # top of the slotted plate
TP_Y1 = 118.0             # slotted top plate reaches here
TP_T = 13.0

# gear motor on -X side of the drive head
GB_X0, GB_X1 = -99.0, -52.0
GB_Y0, GB_Y1 = -44.0, 56.0
GB_Z0, GB_Z1 = 1270.0, 1410.0
GB_ZS = 1318.0            # below this the gearbox is narrower in +Y
GB_Y_LO = 34.0
MOT_X0, MOT_X1 = -132.0, -99.0
MOT_YC, MOT_ZC = 5.2, 1313.0
MOT_S = 76.0
MEC_X0 = -153.0


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_x(x0, x1, y, z, r):
    return (cq.Workplane("YZ").workplane(offset=x0)
            .center(y, z).circle(r).extrude(x1 - x0))


def cyl_z(x, y, z0, z1, r):
    return (cq.Workplane("XY").workplane(offset=z0)
            .center(x, y).circle(r).extrude(z1 - z0))


# ---------------------------------------------------------------------------
# profile
# ---------------------------------------------------------------------------
def make_profile():
    x0, x1, y0, y1 = PROF_X0, PROF_X1, PROF_Y0, PROF_Y1
    cx, cy = PROF_FRONT_CHX, PROF_FRONT_CHY     # bevels on the front corners
    c = PROF_CHAMFER                            # small bevels at the back
    sec = [(x0 + cx, y0), (x1 - cx, y0), (x1, y0 + cy), (x1, y1 - c),
           (x1 - c, y1), (x0 + c, y1), (x0, y1 - c), (x0, y0 + cy)]
    L = Z_PROF1 - Z_PROF0
    p = (cq.Workplane("XY").workplane(offset=Z_PROF0)
         .polyline(sec).close().extrude(L))
    cuts = []
    # two grooves on the -Y (front) face
    xm = (x0 + x1) / 2
    for xc in (xm - FRONT_GROOVE_X, xm + FRONT_GROOVE_X):
        cuts.append(box(xc - GROOVE_W / 2, xc + GROOVE_W / 2,
                        y0 - 1, y0 + GROOVE_D, Z_PROF0 - 1, Z_PROF1 + 1))
    # grooves on the side faces (+X / -X)
    for (yc, w) in PX_GROOVES:
        cuts.append(box(x1 - GROOVE_D, x1 + 1, yc - w / 2, yc + w / 2,
                        Z_PROF0 - 1, Z_PROF1 + 1))
    for (yc, w) in MX_GROOVES:
        cuts.append(box(x0 - 1, x0 + GROOVE_D, yc - w / 2, yc + w / 2,
                        Z_PROF0 - 1, Z_PROF1 + 1))
    # belt slot and T-slot in the rear (+Y) face
    for (sx0, sx1, d) in REAR_SLOTS:
        cuts.append(box(sx0, sx1, y1 - d, y1 + 1, Z_PROF0 - 1, Z_PROF1 + 1))
    for k in cuts:
        p = p.cut(k)
    return p


# ---------------------------------------------------------------------------
# end cap, built for the bottom position (outer end at z=0, body above)
# ---------------------------------------------------------------------------
def flange_on_x(side, zc, lone_angle_deg, boss=True):
    """Bearing flange with 3 screws on the +X (side=1) or -X (side=-1) face:
    thin plate (disc with three screw lugs), screw heads, bearing boss."""
    xf = side * CAP_X / 2
    disk_t, boss_t, head_t = 1.5, 7.0, 3.0
    r_bc = FL_BOLT_R                 # screw circle radius
    x_start = xf if side > 0 else xf - disk_t
    wp = lambda: cq.Workplane("YZ").workplane(offset=x_start)
    y0 = SHAFT_Y
    f = wp().center(y0, zc).circle(FL_R).extrude(disk_t)
    w = 2 * FL_LUG_R
    for k in range(3):
        a = math.radians(lone_angle_deg + 120.0 * k)
        ca, sa = math.cos(a), math.sin(a)
        yy = y0 + r_bc * ca
        zz = zc + r_bc * sa
        # lug: web from the centre plus a round end around the screw
        if FL_LUG_R > 0:
            web = [(y0 - sa * w / 2, zc + ca * w / 2),
                   (yy - sa * w / 2, zz + ca * w / 2),
                   (yy + sa * w / 2, zz - ca * w / 2),
                   (y0 + sa * w / 2, zc - ca * w / 2)]
            f = f.union(wp().polyline(web).close().extrude(disk_t))
            f = f.union(wp().center(yy, zz).circle(FL_LUG_R).extrude(disk_t))
        if side > 0:
            head = cyl_x(xf, xf + disk_t + head_t, yy, zz, 4.5)
            sk = (cq.Workplane("YZ").workplane(offset=xf + disk_t + 1.0)
                  .center(yy, zz).polygon(6, 4.0).extrude(head_t))
        else:
            head = cyl_x(xf - disk_t - head_t, xf, yy, zz, 4.5)
            sk = (cq.Workplane("YZ").workplane(offset=xf - disk_t - head_t - 1)
                  .center(yy, zz).polygon(6, 4.0).extrude(head_t))
        f = f.union(head).cut(sk)
    if boss:
        if side > 0:
            b = cyl_x(xf, xf + boss_t, y0, zc, FL_BOSS_R)
        else:
            b = cyl_x(xf - boss_t, xf, y0, zc, FL_BOSS_R)
        f = f.union(b)
    bt = boss_t if boss else disk_t
    if side > 0:
        hole = (cq.Workplane("YZ").workplane(offset=xf - 10)
                .center(y0, zc).polygon(6, 11.0).extrude(bt + 11))
    else:
        hole = (cq.Workplane("YZ").workplane(offset=xf - bt - 1)
                .center(y0, zc).polygon(6, 11.0).extrude(bt + 11))
    return f.cut(hole)


def dome_solid(z_base, h):
    """Pulley cover on the outer face of a head (bottom orientation: the
    cover hangs below z_base).  Cross shaped footprint with bevelled
    clearance notches around the four corner screws, cylindrical surface
    with its axis along X."""
    y0, y1 = DOME_Y0, DOME_Y1
    hx = CAP_X / 2
    bx = DOME_BAND_X
    w0, w1 = DOME_WIDE_Y
    # one quarter of the notch outline (+X side, going from band to wide)
    lo = [(bx, w0 - 10.0), (bx + 1.5, w0 - 6.8), (bx + 4.6, w0 - 3.8),
          (bx + 13.9, w0)]
    hi = [(bx + 14.2, w1), (bx + 4.6, w1 + 3.7), (bx + 1.5, w1 + 5.6),
          (bx, w1 + 8.8)]
    right = [(bx, y0)] + lo + [(hx, w0), (hx, w1)] + hi + [(bx, y1)]
    left = [(-x, y) for (x, y) in reversed(right)]
    pts = right + left
    foot = (cq.Workplane("XY").workplane(offset=z_base - h)
            .polyline(pts).close().extrude(h))
    yc = (y0 + y1) / 2
    half = (y1 - y0) / 2
    # cylinder through the footprint ends, peaking at height h
    R = (half * half + h * h) / (2 * h)
    zc = z_base - h + R
    c = cyl_x(-hx - 1, hx + 1, yc, zc, R)
    return foot.intersect(c)


def make_cap(body_h, dome_h, shaft_u, lone_angle, flange_minus_x, hole_y):
    """End cap built in bottom orientation: outer face of the block at
    z=dome_h, cover below it down to z=0, block up to dome_h+body_h."""
    z0 = dome_h
    body = box(-CAP_X / 2, CAP_X / 2, -CAP_Y / 2, CAP_Y / 2, z0, z0 + body_h)
    body = body.faces("<Z").edges().chamfer(CAP_TOP_CHAMFER)
    body = body.faces(">Z").edges().chamfer(1.5)
    body = body.edges("|Z").chamfer(1.5)
    # recess on -Y face
    rec = (cq.Workplane("XZ").workplane(offset=CAP_Y / 2 - RECESS_D)
           .center((RECESS_X0 + RECESS_X1) / 2,
                   z0 + (RECESS_U0 + RECESS_U1) / 2)
           .rect(RECESS_X1 - RECESS_X0, RECESS_U1 - RECESS_U0)
           .extrude(RECESS_D + 1))
    rec = rec.edges("|Y").fillet(5.0)
    body = body.cut(rec)
    # corner screws in the outer face: square (diamond) sockets
    for sx in (-CAP_SCREW_X, CAP_SCREW_X):
        for sy in (-CAP_SCREW_Y, CAP_SCREW_Y):
            sock = (cq.Workplane("XY").workplane(offset=z0 - 1.0)
                    .center(sx, sy).rect(7.0, 7.0).extrude(5.0)
                    .rotate((sx, sy, 0), (sx, sy, 1), 45))
            body = body.cut(sock)
    # two small holes on the +X face near the +Y edge
    for zz in (z0 + 12.0, z0 + 78.0):
        body = body.cut(cyl_x(CAP_X / 2 - 6, CAP_X / 2 + 1, hole_y, zz, 2.0))
    cap = body.union(dome_solid(z0, dome_h))
    zc = z0 + shaft_u
    cap = cap.union(flange_on_x(1, zc, lone_angle, boss=True))
    if flange_minus_x:
        cap = cap.union(flange_on_x(-1, zc, lone_angle, boss=False))
    return cap


# ---------------------------------------------------------------------------
# front mounting plate and small bracket (on -Y face of profile)
# ---------------------------------------------------------------------------
def make_plates():
    yb = PROF_Y0
    plate = box(PLATE_X0, PLATE_X1, yb - PLATE_T, yb, PLATE_Z0, PLATE_Z1)
    plate = plate.edges("|Y").fillet(4.0)
    brk = box(BRK_X0, BRK_X1, yb - PLATE_T, yb, BRK_Z0, BRK_Z1)
    brk = brk.edges("|Y").fillet(3.0)
    res = plate.union(brk)
    # holes + screw heads
    holes_small = [(-178.0, 1235.0), (-178.0, 1122.0),
                   (-100.0, 1073.0), (-100.0, 1036.0)]
    for (x, z) in holes_small:
        h = (cq.Workplane("XZ").workplane(offset=-yb - 1)
             .center(x, z).circle(2.5).extrude(PLATE_T + 2))
        res = res.cut(h)
    heads = [(-33.0, 1235.0), (-33.0, 1122.0), (-31.0, 1075.0), (-31.0, 1035.0)]
    yf = yb - PLATE_T          # outer face of the plates
    for (x, z) in heads:
        # low button head with hex socket
        ring = (cq.Workplane("XZ").workplane(offset=-yf - 1.0)
                .center(x, z).circle(6.0).circle(5.0).extrude(2.0))
        res = res.cut(ring)
        sk = (cq.Workplane("XZ").workplane(offset=-yf - 1.0)
              .center(x, z).polygon(6, 5.0).extrude(4.0))
        res = res.cut(sk)
    return res


# ---------------------------------------------------------------------------
# tensioner block on +Y of the drive head
# ---------------------------------------------------------------------------
def make_tensioner():
    z_top = TP_Z1
    tb = box(-TB_X / 2, TB_X / 2, TB_Y0, TB_Y1, TB_Z0, z_top - TP_T)
    tp = box(-CAP_X / 2, CAP_X / 2, TB_Y0, TP_Y1, z_top - TP_T, z_top)
    tp = tp.edges("|Z").fillet(3.0)
    t = tb.union(tp)
    # slots in the top plate
    for xs in (-32.6, 32.6):
        sl = (cq.Workplane("XY").workplane(offset=z_top - TP_T - 1)
              .center(xs, 92.5).slot2D(41.0, 8.0, angle=90)
              .extrude(TP_T + 2))
        t = t.cut(sl)
        t = t.union(cyl_z(xs, 76.0, z_top - TP_T - 1, z_top - 2.0, 3.5))
    # elongated hexagonal nut pockets with slotted screws on the side faces
    zc = 1370.0
    yc = 73.0
    hw, hh = 14.0, 21.0
    hex_pts = [(yc, zc + hh), (yc + hw, zc + hh / 2), (yc + hw, zc - hh / 2),
               (yc, zc - hh), (yc - hw, zc - hh / 2), (yc - hw, zc + hh / 2)]
    for side in (1, -1):
        xf = side * TB_X / 2
        x_in = xf - 4.0 if side > 0 else xf - 1.0
        hx = (cq.Workplane("YZ").workplane(offset=x_in)
              .polyline(hex_pts).close().extrude(5.0))
        t = t.cut(hx)
        if side > 0:
            scr = cyl_x(xf - 4.0, xf - 1.0, yc, zc, 10.0)
            slot = box(xf - 2.5, xf, yc - 10.5, yc + 10.5, zc - 1.2, zc + 1.2)
        else:
            scr = cyl_x(xf + 1.0, xf + 4.0, yc, zc, 10.0)
            slot = box(xf, xf + 2.5, yc - 10.5, yc + 10.5, zc - 1.2, zc + 1.2)
        t = t.union(scr).cut(slot)
    # two small studs below the block
    for ys in (60.0, 82.0):
        t = t.union(cyl_z(30.0, ys, 1313.0, TB_Z0 + 1, 8.0))
    return t


# ---------------------------------------------------------------------------
# gear motor on -X of the drive head
# ---------------------------------------------------------------------------
def make_motor():
    # gearbox housing: section in the YZ plane extruded along X.  Full width
    # at the top (next to the head), recessed and bevelled below it.
    sec = [(GB_Y0 + 12.0, GB_Z0), (GB_Y_LO, GB_Z0), (GB_Y_LO, GB_ZS),
           (GB_Y1, GB_ZS + 16.0), (GB_Y1, GB_Z1), (GB_Y0, GB_Z1),
           (GB_Y0, GB_Z1 - 28.0), (GB_Y0 + 12.0, GB_Z1 - 60.0)]
    g = (cq.Workplane("YZ").workplane(offset=GB_X0)
         .polyline(sec).close().extrude(GB_X1 - GB_X0))
    # adapter flange between gearbox and head (same section, slightly inset)
    fl = (cq.Workplane("YZ").workplane(offset=GB_X1)
          .polyline(sec).close().extrude(-CAP_X / 2 - GB_X1))
    # shallow steps on the motor side of the gearbox top
    g = g.cut(box(GB_X0 - 1, -74.0, GB_Y0 - 1, GB_Y0 + 8.5, GB_Z1 - 5, GB_Z1 + 1))
    g = g.cut(box(GB_X0 - 1, -74.0, GB_Y1 - 9.5, GB_Y1 + 1, GB_Z1 - 5, GB_Z1 + 1))
    # oblong inspection cover on top of the gearbox
    ob = (cq.Workplane("XY").workplane(offset=GB_Z1 - 2.0)
          .center(-93.0, 6.0).slot2D(32.0, 9.0, angle=90).extrude(2.5))
    g = g.cut(ob)
    # two holes on the motor side face of the gearbox (above the motor)
    for yy in (-8.0, 24.0):
        g = g.cut(cyl_x(GB_X0 - 1, GB_X0 + 8, yy, 1378.0, 4.0))
    g = g.union(fl)
    # motor body (square)
    m = box(MOT_X0, MOT_X1, MOT_YC - MOT_S / 2, MOT_YC + MOT_S / 2,
            MOT_ZC - MOT_S / 2, MOT_ZC + MOT_S / 2)
    m = m.edges("|X").chamfer(5.0)
    # motor end cap (encoder cover), rounded
    mc = box(MEC_X0, MOT_X0, MOT_YC - 40.0, MOT_YC + 41.0,
             MOT_ZC - MOT_S / 2 - 4.0, MOT_ZC + MOT_S / 2 + 6.0)
    mc = mc.edges("|X").fillet(6.0)
    mc = mc.faces("<X").edges().fillet(7.0)
    # connector on top of the end cap
    con = box(-151.0, -135.0, -10.0, 21.0,
              MOT_ZC + MOT_S / 2 + 4.0, MOT_ZC + MOT_S / 2 + 18.0)
    con = con.edges("|Y").fillet(5.0)
    # four contact pins visible in the connector top
    for k in range(4):
        con = con.cut(cyl_z(-143.0, -1.0 + 4.5 * k, MOT_ZC + MOT_S / 2 + 14.0,
                            MOT_ZC + MOT_S / 2 + 19.0, 1.0))
    return g.union(m).union(mc).union(con)


profile = make_profile()
cap_bot = make_cap(BOT_BODY_H, BOT_DOME_H, BOT_SHAFT_U, 0.0, True, 38.0)
# the drive head has its single screw towards -Y
cap_top = (make_cap(TOP_BODY_H, TOP_DOME_H, TOP_SHAFT_U, 180.0, False, -38.0)
           .mirror("XY").translate((0, 0, H_TOTAL)))
plates = make_plates()
tens = make_tensioner()
motor = make_motor()

result = (profile.union(cap_bot).union(cap_top).union(plates)
          .union(tens).union(motor))

VIEW = {"azimuth": 45, "elevation": 26}
